import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# The part is a solid of revolution about the global X axis.
# x = 0 at the centre of the left (small-end) ball.
L_BALL_R = 7.0           # left ball radius
L_BALL_X = 0.25          # left ball centre (its tip sits at x = -6.75)
NECK_R = 2.85            # thin neck radius carrying the ribs

RIB_T = 2.9              # rib (disc) thickness along the axis
RIB_X0 = 12.85           # centre of the first (smallest) rib
RIB_PITCH = 5.65         # rib spacing along the axis
RIB_R = [6.5, 7.6, 9.85, 11.8]          # rib outer radii, small end to large end

FLANGE_X = 37.25         # flange centre position
FLANGE_T = 6.2           # flange thickness
FLANGE_R = 15.5          # flange outer radius

CAP_RATIO = 2.0          # radial / axial semi-axis of the elliptical rim rounding
RIM_ANGLES = (25, 50, 70, 85)   # sample angles (deg) along the elliptical rim

SHAFT_R = 5.925          # main shaft radius
STEP_X = 82.35           # end of main shaft / start of reduced pin
PIN_R = 4.55             # reduced pin radius
R_BALL_X = 105.2         # right ball centre
R_BALL_R = 6.35          # right ball radius

SEAM_ANGLE = -35.0       # angular position (about X) of the revolve seam, hidden at back-bottom


def side_pts(a, R, r_in):
    """Points (dx, r) of one disc side, from the core radius r_in to the rim tip:
    a flat face (dx = a) blending into an elliptical rim of semi-axes a (axial)
    and b = CAP_RATIO * a (radial)."""
    b = CAP_RATIO * a
    r_j = max(R - b, r_in)
    pts = [(a, r_in)]
    if r_j - r_in > 4.0:
        pts.append((a, 0.5 * (r_in + r_j)))
    if r_j - r_in > 0.2:
        pts.append((a, r_j))
    for d in RIM_ANGLES:
        t = math.radians(d)
        pts.append((a * math.cos(t), r_j + (R - r_j) * math.sin(t)))
    pts.append((0.0, R))
    return pts


def disc(wp, xc, t, R, r_right, r_left):
    """Rounded disc centred at xc, traced right-to-left over its rim, sitting on a
    core of radius r_right (right face) / r_left (left face).  Each side is one
    smooth spline face; the two sides meet at the rim equator."""
    a = t / 2.0
    pr = side_pts(a, R, r_right)
    pl = side_pts(a, R, r_left)
    wp = wp.lineTo(xc + pr[0][0], pr[0][1])
    up = [(xc + dx, r) for dx, r in pr[1:]]
    wp = wp.spline(up, tangents=[(0.0, 1.0), (-1.0, 0.0)], includeCurrent=True)
    down = [(xc - dx, r) for dx, r in reversed(pl[:-1])]
    wp = wp.spline(down, tangents=[(-1.0, 0.0), (0.0, -1.0)], includeCurrent=True)
    return wp


# ---------------- profile (upper half, traced right to left) ----------------
# right ball: from its tip on the axis to the pin junction
th_r = math.pi - math.asin(PIN_R / R_BALL_R)
_c, _s = math.cos(math.radians(SEAM_ANGLE)), math.sin(math.radians(SEAM_ANGLE))
# sketch plane contains the X axis; its local +y (the radial direction of the
# profile) points at SEAM_ANGLE around X, which is where the revolve seam ends up
SKETCH = cq.Plane(origin=(0, 0, 0), xDir=(1, 0, 0), normal=(0, -_s, _c))
prof = cq.Workplane(SKETCH).moveTo(R_BALL_X + R_BALL_R, 0.0)
prof = prof.threePointArc(
    (R_BALL_X + R_BALL_R * math.cos(th_r / 2.0), R_BALL_R * math.sin(th_r / 2.0)),
    (R_BALL_X + R_BALL_R * math.cos(th_r), PIN_R),
)
# pin, step, main shaft
prof = prof.lineTo(STEP_X, PIN_R).lineTo(STEP_X, SHAFT_R)

# flange between main shaft (right) and neck (left)
prof = disc(prof, FLANGE_X, FLANGE_T, FLANGE_R, SHAFT_R, NECK_R)

# ribs on the neck, largest first
RIB_X = [RIB_X0 + i * RIB_PITCH for i in range(len(RIB_R))]
for x, r in reversed(list(zip(RIB_X, RIB_R))):
    prof = disc(prof, x, RIB_T, r, NECK_R, NECK_R)

# left ball: from the neck junction to its tip on the axis
th_l = math.asin(NECK_R / L_BALL_R)
prof = prof.lineTo(L_BALL_X + L_BALL_R * math.cos(th_l), NECK_R)
th_m = 0.5 * (th_l + math.pi)
prof = prof.threePointArc(
    (L_BALL_X + L_BALL_R * math.cos(th_m), L_BALL_R * math.sin(th_m)),
    (L_BALL_X - L_BALL_R, 0.0),
)
prof = prof.close()

# revolve about the (global) X axis
result = prof.revolve(360, (0, 0, 0), (1, 0, 0))

VIEW = {"azimuth": 45, "elevation": 26}
